import cadquery as cq

# Downtown city-block model: a thin ground plate with extruded building masses.
# Plan coordinates are given in "sheet" units (sx, sy): x to the right, y DOWN the page
# of the plan; S() converts them to model XY (mm). Heights in mm above the ground plate.

PLATE_T = 1.0

def S(sx, sy):
    return (sx - 130.0, 390.0 - sy)

plate_pts = [S(22.5, 298.5), S(206.3, 298.5), S(206.3, 475.5), S(200.3, 464.0),
             S(148.6, 481.3), S(22.5, 481.3)]

def R(x0, y0, x1, y1):
    return [(x0, y0), (x1, y0), (x1, y1), (x0, y1)]

# (footprint polygon in plan units, top height)
BUILDINGS = [
    # ---- north-west: slab A and its wings
    ([(44.6, 275.4), (60.9, 282.8), (58.3, 307.9), (35.9, 301.0)], 30.0),
    ([(60.9, 282.8), (71.3, 287.9), (58.3, 307.9)], 20.0),
    ([(35.9, 301.0), (58.3, 307.9), (47.0, 326.5), (30.3, 319.6)], 30.0),
    ([(30.3, 319.6), (47.0, 326.5), (46.5, 336.2), (26.3, 330.4)], 16.4),
    ([(23.0, 353.0), (29.5, 350.5), (31.5, 358.0), (25.0, 360.5)], 8.0),
    # ---- north-middle: slab B, ziggurat, block C
    ([(86.7, 283.3), (106.9, 294.8), (104.6, 298.3), (83.8, 289.0)], 52.3),
    ([(83.8, 289.0), (104.6, 298.3), (101.2, 309.8), (79.8, 301.2)], 44.1),
    ([(111.0, 294.0), (121.3, 293.5), (120.8, 287.7), (134.0, 287.1), (134.0, 321.0), (111.0, 321.0)], 20.0),
    (R(115.9, 299.5, 128.5, 313.5), 46.2),
    # ---- block between the two cross streets (middle)
    (R(97.9, 328.0, 133.5, 339.6), 14.0),
    ([(82.8, 334.0), (92.8, 332.7), (95.6, 358.0), (85.4, 359.6)], 37.4),
    (R(95.6, 342.8, 114.4, 362.3), 22.0),
    (R(117.1, 348.2, 129.9, 365.7), 37.0),
    (R(107.7, 355.6, 116.4, 365.0), 18.0),
    (R(83.5, 370.4, 103.0, 385.2), 24.0),
    (R(102.3, 371.7, 111.7, 383.8), 38.0),
    (R(112.4, 371.0, 129.2, 385.9), 29.2),
    # ---- south-middle
    ([(93.5, 390.6), (108.7, 390.6), (108.7, 397.3), (88.0, 403.6), (86.5, 396.5)], 39.0),
    (R(86.5, 390.6, 93.8, 394.4), 30.0),
    ([(90.4, 410.0), (101.0, 408.8), (102.9, 422.5), (92.0, 424.2)], 20.0),
    ([(103.8, 407.0), (115.4, 404.5), (117.0, 416.5), (105.2, 418.5)], 24.0),
    ([(116.0, 403.0), (128.0, 400.0), (129.5, 411.5), (117.5, 414.6)], 27.1),
    # ---- D - big slab south-west, with low annex in front
    ([(99.4, 444.2), (133.1, 437.5), (135.8, 454.3), (102.8, 461.1)], 58.0),
    ([(106.2, 460.4), (134.4, 455.7), (135.1, 464.4), (107.5, 469.8)], 21.0),
    # ---- west column
    (R(48.7, 390.9, 73.0, 404.8), 46.2),
    (R(67.5, 413.0, 81.4, 435.6), 42.6),
    (R(57.8, 425.0, 67.5, 437.2), 12.0),
    ([(45.2, 384.4), (49.0, 351.0), (74.0, 351.0), (77.5, 384.4)], 6.0),
    # ---- north-east
    ([(149.6, 273.5), (187.7, 291.9), (187.0, 300.0), (142.7, 300.0), (143.8, 291.9)], 28.5),
    ([(141.0, 307.0), (159.0, 307.0), (159.7, 316.5), (142.0, 316.5)], 36.0),
    ([(139.8, 316.5), (164.6, 316.5), (164.6, 320.5), (139.8, 320.5)], 18.0),
    ([(167.0, 308.0), (177.0, 300.0), (182.0, 303.0), (178.0, 313.0), (167.5, 317.0)], 46.0),
    ([(191.7, 320.1), (217.3, 316.1), (219.3, 326.2), (194.4, 330.9)], 29.0),
    ([(139.1, 326.7), (152.0, 326.7), (152.6, 340.0), (150.0, 353.2), (139.1, 353.2)], 39.5),
    ([(150.2, 333.5), (166.5, 333.5), (166.5, 345.0), (150.2, 345.0)], 14.0),
    ([(178.9, 336.2), (185.7, 326.1), (190.4, 330.2), (183.0, 342.3)], 15.0),
    ([(160.8, 350.4), (178.3, 340.3), (183.0, 347.0), (164.8, 358.5)], 10.0),
    ([(163.5, 363.8), (182.3, 353.1), (186.3, 358.5), (167.5, 370.6)], 10.0),
    ([(183.0, 344.0), (195.0, 339.0), (199.8, 349.0), (187.0, 355.8)], 15.0),
    ([(184.0, 366.0), (200.0, 352.0), (213.0, 362.0), (197.0, 380.0)], 26.0),
    ([(137.7, 359.6), (153.1, 358.2), (160.8, 377.9), (138.7, 382.7)], 40.0),
    # ---- south-east
    ([(184.6, 402.3), (201.5, 390.8), (222.8, 421.2), (212.3, 432.3)], 62.7),
    ([(201.0, 393.0), (207.7, 386.9), (222.3, 375.4), (248.6, 404.8), (223.0, 421.0)], 6.5),
    ([(137.7, 394.0), (163.0, 389.5), (164.6, 400.8), (138.5, 405.4)], 19.0),
    ([(143.8, 420.8), (176.2, 415.4), (178.5, 433.1), (147.7, 438.5)], 28.0),
    ([(154.0, 438.6), (179.0, 433.9), (181.7, 450.0), (157.2, 454.8)], 46.3),
]

def prism(pts, h, z0=0.0):
    return (cq.Workplane("XY").workplane(offset=z0)
            .polyline([S(*p) for p in pts]).close().extrude(h - z0))

result = cq.Workplane("XY").polyline(plate_pts).close().extrude(-PLATE_T)
for pts, h in BUILDINGS:
    result = result.union(prism(pts, h))

# tower G: stepped wedge base, collar and octagonal shaft
gx, gy = S(197.7, 304.2)
result = result.union(prism([(191.0, 296.5), (214.2, 308.0), (191.0, 312.7)], 20.5))
result = result.union(prism([(192.5, 298.0), (209.0, 306.5), (192.5, 311.0)], 26.5, 20.5))
result = result.union(cq.Workplane("XY").workplane(offset=26.5).center(gx, gy).polygon(8, 14.4).extrude(4.5))
result = result.union(cq.Workplane("XY").workplane(offset=31.0).center(gx, gy).polygon(8, 11.6).extrude(37.0))
# round building (rounded SW corner)
rb = (cq.Workplane("XY").center(*S(52.85, 418.65)).rect(14.9, 14.3).extrude(46.6)
      .edges("|Z").edges("<X").fillet(7.0))
result = result.union(rb)
# ziggurat tower
zc = S(88.8, 311.5)
for (w, d, z0, z1) in [(20, 16, 0, 24), (15, 12, 24, 32), (12, 10, 32, 40), (9, 8, 40, 44), (5, 5, 44, 47.4)]:
    result = result.union(cq.Workplane("XY").workplane(offset=z0).center(*zc).rect(w, d).extrude(z1 - z0)
                          .rotate((zc[0], zc[1], 0), (zc[0], zc[1], 1), -20))
# rooftop plant boxes
result = result.union(prism(R(50.6, 413.5, 58.8, 420.7), 49.7, 40.0))
result = result.union(prism([(161.0, 440.5), (170.5, 438.8), (172.0, 447.0), (162.5, 448.7)], 47.8, 40.0))
result = result.union(prism([(170.0, 304.0), (175.0, 302.0), (176.0, 307.0), (171.0, 309.0)], 48.0, 40.0))
# SW pier blob and access ramps (for the overall extents)
result = result.union(prism([(11.5, 484.1), (16, 477), (23, 478), (25, 484), (19, 492), (15, 496)], 3.5, -PLATE_T))
result = result.union(prism([(84, 480), (88, 480), (103.5, 505), (101.0, 506.5)], 0.0, -PLATE_T))
result = result.union(prism([(73.4, 480.0), (77.0, 480.0), (69.5, 492.0), (67.0, 499.2), (63.8, 490.8), (63.1, 487.6)], 0.0, -PLATE_T))
